import math
import cadquery as cq

# Toy-style wheel: octagonal tread band with diamond lugs between two bevelled
# side plates; the outer face carries six flat-topped spokes with ridged noses,
# conical-floored grooves between them and a domed hub with a D bore.
# Wheel axis = global X, spoke field facing +X, plain back face towards -X.

# ---------------- driving dimensions (mm) ----------------
R_PLATE = 57.5        # radius of the two side plates
W_RIM = 22.3          # axial width between the two plate rims (tips)
APOTHEM = 52.0        # octagonal tread band: distance to the flats
PLATE_EDGE = 0.25     # plate thickness at its outer edge
BEVEL_R = 52.0        # inner bevel of the plates: reference radius ...
FRONT_BEVEL = 1.45    # ... and how far behind the rim it is there (front)
BACK_BEVEL = 1.65     # (back plate)
BACK_BULGE = 0.8      # back face is a flat cone, this much proud at the centre
FRONT_DROP = 1.1      # front ring face falls this much from R_FIELD to the rim

R_FIELD = 53.0        # inner radius of the front ring (spoke field)
FIELD_REC = 0.0       # spoke tops sit this far below the ring's inner edge

N_SPOKES = 6
SPOKE_ANG0 = 30.0     # first spoke direction, degrees from +Y towards +Z
SPOKE_HALF_ANG = 15.0 # spokes are radial sectors of this half angle
WALL_DRAFT = 8.0      # lean of the spoke side walls (deg from the axis)
V_R_EDGE = 33.0       # nose flanks start on the spoke edges here
V_R_TIP = 24.6        # ... and on the spoke centre line here
NOSE_H = 1.0          # flank height above the floor at the hub radius

DISH_H0 = 1.0         # groove floor height above the hub floor at the hub radius

HUB_R = 14.0
HUB_TOP = 4.2         # axial position of the hub crown
HUB_BASE = 2.2        # axial position where the hub dome meets its side
HUB_FLOOR_H = 1.6     # hub side height above the surrounding floor
HUB_FILLET = 2.0
CBORE_R = 7.0         # conical countersink in the hub face
CBORE_D = 2.0
BORE_R = 3.0
BORE_FLAT = 2.4       # D bore: distance from centre to the flat
BACK_BOSS_R = 8.0
BACK_BOSS_H = 0.7

N_LUGS = 8
LUG_L0, LUG_W0 = 25.5, 7.7   # diamond base (tangential x axial)
LUG_L1, LUG_W1 = 13.0, 4.75  # diamond top
LUG_H = 7.5                  # lug height above the flat
LUG_H0 = 3.3                 # height of the straight-sided part

X1 = 12.0                      # front face (spoke tops / ring inner edge)
X_RIM_F = X1 - FRONT_DROP      # front plate rim
X0 = X_RIM_F - W_RIM           # back plate rim
X_MID = 0.5 * (X0 + X_RIM_F)   # mid plane of the tread band
X_T = X1 - FIELD_REC           # spoke top level
X_FLOOR = HUB_BASE - HUB_FLOOR_H  # floor level around the hub


def revolve_x(pts):
    """Revolve a closed (x, r) profile about the global X axis."""
    return cq.Workplane("XY").polyline(pts).close().revolve(360.0, (0, 0, 0), (1, 0, 0))


def rot(r, t, ang):
    """(radial, tangential) in a frame turned by ang (rad) about X -> (Y, Z)."""
    c, s = math.cos(ang), math.sin(ang)
    return (r * c - t * s, r * s + t * c)


def disc(x_from, x_to, r):
    return cq.Workplane("YZ", origin=(x_from, 0, 0)).circle(r).extrude(x_to - x_from)


# ---------------- side plates with bevelled rims ----------------
def plate(x_rim, sgn, bevel):
    """Side plate; sgn = +1 for the front plate, -1 for the back plate.
    Its inner face is a cone that thins the plate to a sharp rim."""
    k = bevel / (R_PLATE - BEVEL_R)
    r_in = BEVEL_R - 6.0
    return revolve_x([
        (x_rim + sgn * 3.0, 0), (x_rim + sgn * 3.0, R_PLATE), (x_rim, R_PLATE),
        (x_rim - sgn * PLATE_EDGE, R_PLATE),
        (x_rim - sgn * (PLATE_EDGE + k * (R_PLATE - r_in)), r_in),
        (x_rim - sgn * (PLATE_EDGE + k * (R_PLATE - r_in)), 0)])


# ---------------- octagonal tread band ----------------
r_corner = APOTHEM / math.cos(math.pi / 8)
oct_pts = [(r_corner * math.cos(math.pi / 8 + k * math.pi / 4),
            r_corner * math.sin(math.pi / 8 + k * math.pi / 4)) for k in range(8)]
band = (cq.Workplane("YZ", origin=(X0 - 2.0, 0, 0)).polyline(oct_pts).close()
        .extrude(X1 - X0 + 4.0))

body = band.union(plate(X0, -1, BACK_BEVEL)).union(plate(X_RIM_F, 1, FRONT_BEVEL))

# outer faces: a flat cone on the back, flat centre and conical ring in front
body = body.cut(revolve_x([
    (X1, 0), (X1, R_FIELD), (X_RIM_F, R_PLATE), (X_RIM_F, R_PLATE + 20.0),
    (X1 + 10.0, R_PLATE + 20.0), (X1 + 10.0, 0)]))
body = body.cut(revolve_x([
    (X0 - BACK_BULGE, 0), (X0, R_PLATE), (X0, R_PLATE + 20.0),
    (X0 - 10.0, R_PLATE + 20.0), (X0 - 10.0, 0)]))

# ---------------- spoke field inside the front ring ----------------
tan_s = math.tan(math.radians(SPOKE_HALF_ANG))
# octagon prism slightly inside the tread band: keeps every cut off the flats
oct_in = [(x * (APOTHEM - 0.6) / APOTHEM, y * (APOTHEM - 0.6) / APOTHEM) for x, y in oct_pts]
inner_prism = (cq.Workplane("YZ", origin=(X0 - 2.0, 0, 0)).polyline(oct_in).close()
               .extrude(X1 - X0 + 4.0))

# optional shallow recess: spoke tops a little below the ring's inner edge
if FIELD_REC > 0:
    body = body.cut(disc(X_T, X1 + 1.0, R_FIELD).intersect(inner_prism))


def halfspace_box(origin, x_dir, normal, inside):
    """Large box on the side of the plane (origin, normal) that holds 'inside'."""
    if normal.dot(inside - origin) < 0:
        normal = -normal
    return cq.Workplane(cq.Plane(origin=origin, xDir=x_dir, normal=normal)).rect(
        400.0, 400.0).extrude(150.0)


def spoke_outline(ang, x_from, x_to):
    """Region of one spoke: a radial sector whose side walls lean out with
    WALL_DRAFT towards the floor (the spoke is wider at its root)."""
    tan_d = math.tan(math.radians(WALL_DRAFT))
    o = cq.Vector(X_T, 0, 0)
    inside = cq.Vector(X_T - 1.0, 30.0 * math.cos(ang), 30.0 * math.sin(ang))
    reg = disc(x_from, x_to, R_FIELD + 5.0)
    for side in (-1, 1):
        phi = ang + side * math.radians(SPOKE_HALF_ANG)
        l_dir = cq.Vector(0, math.cos(phi), math.sin(phi))
        e_t = cq.Vector(0, -math.sin(phi), math.cos(phi)) * side
        d_dir = cq.Vector(-1, 0, 0) + e_t * tan_d
        reg = reg.intersect(halfspace_box(o, l_dir, l_dir.cross(d_dir), inside))
    return reg


# groove floor between the spokes: a cone from the ring's inner edge down to the hub
dish = revolve_x([
    (X1 + 1.0, 0), (X1 + 1.0, R_FIELD), (X_T, R_FIELD),
    (X_FLOOR + DISH_H0, HUB_R), (X_FLOOR + DISH_H0, 0)])
above_floor = dish
for i in range(N_SPOKES):
    dish = dish.cut(spoke_outline(math.radians(SPOKE_ANG0 + i * 360.0 / N_SPOKES),
                                  X_FLOOR - 5.0, X1 + 5.0))
body = body.cut(dish)

# ridged noses: two sloping flanks on every spoke towards the hub
for i in range(N_SPOKES):
    ang = math.radians(SPOKE_ANG0 + i * 360.0 / N_SPOKES)
    for side in (-1, 1):
        y1, z1 = rot(V_R_EDGE, side * V_R_EDGE * tan_s, ang)
        y2, z2 = rot(V_R_TIP, 0.0, ang)
        y3, z3 = rot(HUB_R, side * HUB_R * tan_s, ang)
        p1 = cq.Vector(X_T, y1, z1)
        p2 = cq.Vector(X_T, y2, z2)
        p3 = cq.Vector(X_FLOOR + NOSE_H, y3, z3)
        n = (p2 - p1).cross(p3 - p1)
        yc, zc = rot(0.5 * (V_R_EDGE + HUB_R), 0.0, ang)
        if n.dot(cq.Vector(X_FLOOR, yc, zc) - p1) > 0:
            n = -n
        half_space = cq.Workplane(cq.Plane(origin=p1, xDir=(p2 - p1), normal=n)).rect(
            200.0, 200.0).extrude(60.0)
        body = body.cut(half_space.intersect(spoke_outline(ang, X_FLOOR - 5.0, X1 + 5.0))
                        .intersect(disc(X_FLOOR - 5.0, X1 + 5.0, V_R_EDGE + 2.0))
                        .intersect(above_floor))

# ---------------- domed hub with D bore, back boss ----------------
hub = (disc(X_FLOOR - 1.0, HUB_TOP, HUB_R).faces(">X").edges().fillet(HUB_FILLET)
       .cut(revolve_x([(HUB_TOP + 1.0, 0), (HUB_TOP + 1.0, CBORE_R), (HUB_TOP, CBORE_R),
                       (HUB_TOP - CBORE_D, BORE_R), (HUB_TOP - CBORE_D, 0)])))
x_boss = X0 - BACK_BULGE * (1.0 - BACK_BOSS_R / R_PLATE)
boss = disc(x_boss - BACK_BOSS_H, x_boss + 2.0, BACK_BOSS_R)
body = body.union(hub).union(boss)
bore = (disc(X0 - 5.0, X1 + 5.0, BORE_R)
        .intersect(cq.Workplane("YZ", origin=(X0 - 6.0, 0, 0)).center(0, 10.0 - BORE_FLAT)
                   .rect(30.0, 20.0).extrude(X1 - X0 + 12.0)))
body = body.cut(bore)


# ---------------- diamond lugs on the octagon flats ----------------
def rhombus(w, l):
    return [(w / 2, 0), (0, l / 2), (-w / 2, 0), (0, -l / 2)]


def lug():
    """Diamond lug: straight-sided base block topped by a tapering crown."""
    base = (cq.Workplane("XY", origin=(X_MID, 0, APOTHEM - 0.5)).polyline(rhombus(LUG_W0, LUG_L0))
            .close().extrude(LUG_H0 + 0.5))
    crown = (cq.Workplane("XY", origin=(X_MID, 0, APOTHEM + LUG_H0)).polyline(rhombus(LUG_W0, LUG_L0))
             .close().workplane(offset=LUG_H - LUG_H0).polyline(rhombus(LUG_W1, LUG_L1)).close()
             .loft(ruled=True))
    return base.union(crown)


l0 = lug()
for k in range(N_LUGS):
    body = body.union(l0.rotate((0, 0, 0), (1, 0, 0), k * 360.0 / N_LUGS))

result = body

VIEW = {"azimuth": 45, "elevation": 26}
